import cadquery as cq
import math
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# ---------------------------------------------------------------
# Two-piece clamp / tube holder (two separate bodies side by side)
# All dimensions in millimetres
# ---------------------------------------------------------------
L = 22.1            # length of each body along X
PLATE_HW = 8.25     # half width (Y) of the main plate
TAB_HW = 13.6       # half width (Y) over the end tabs
T_PLATE = 3.1       # plate thickness
T_TAB = 3.65        # height of the end tabs
TAB_X0 = 13.3       # X where the end tabs start
CORNER_R = 1.55     # rounding of the plate / arm corners (plan view)
TAB_CORNER_R = 2.75 # rounding of the tab outer corner (plan view)
TAB_BOTTOM_R = 3.1  # rounding of the tab lower front edge
TAB_EDGE_R = 0.75   # round on the tab outer lower edge

HOLE_D = 3.5        # screw hole diameter
HOLE_X = 7.6        # screw hole X position
HOLE_Y = 6.25       # screw hole Y offset from body centre

CHAN_X0 = 16.8      # start of the tube channel
CHAN_R = 4.45       # radius of the tube channel (axis along X)
CHAN_ZC = T_TAB     # channel axis height

TROUGH_X0 = 12.1    # start of the small trough (back body)
TROUGH_R = 2.375    # radius of the small trough

GROOVE_XC = 20.125  # transverse snap groove on the tab (axis along Y)
GROOVE_R = 1.4      # its radius
GROOVE_DZ = 0.83    # its axis lies below the tab top (undercut opening)
OUTER_LIP = 0.9     # outer wall left at the groove end
XGROOVE_R = 1.3     # small groove through the end lip (axis along X)
XGROOVE_Y = 10.5    # its |Y| offset from body centre
XGROOVE_DZ = 0.2    # its axis sits this far below the tab top

NUT_AF = 5.5        # hex nut trap across flats (M3 nut, back body underside)
NUT_DEPTH = 1.4

ARM_GAP_HW = 4.2    # half width of the slot between the arms (front body)
ARM_INNER_R = 0.3   # small rounding of the inner arm tips
POCKET_X0 = 6.8     # recess in front body
POCKET_HW = 7.5
FLOOR_T = 0.8

BODY_SPACING = 32.0  # centre distance (Y) between the two bodies

# engraved letter "R" on the underside of both bodies
R_H = 8.2           # letter height (along -X)
R_W = 5.6           # letter width (along -Y)
R_T = 1.3           # stroke width
R_DEPTH = 0.3       # engraving depth
R_XC = 12.1         # letter centre, measured from the -X end

X0 = -L / 2.0        # part starts here in X


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_x(x0, x1, yc, zc, r):
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .center(yc, zc).circle(r).extrude(x1 - x0))


def cyl_y(y0, y1, xc, zc, r):
    return (cq.Workplane("XZ", origin=(0, y1, 0))
            .center(xc, zc).circle(r).extrude(y1 - y0))


def tab(yc, side):
    """End tab on side (+1/-1) of a body centred at yc."""
    yi = yc + side * PLATE_HW
    yo = yc + side * TAB_HW
    y0, y1 = min(yi, yo), max(yi, yo)
    x0, x1 = X0 + TAB_X0, X0 + L
    t = box(x0, x1, y0, y1, 0, T_TAB)
    # round the outer vertical corner and the lower front edge together
    # (two radii in one fillet operation, so they blend into each other)
    e_vert = t.edges("|Z").edges(
        cq.selectors.NearestToPointSelector((x0, yo, T_TAB / 2))).val()
    e_bot = t.edges("|Y").edges(
        cq.selectors.NearestToPointSelector((x0, (y0 + y1) / 2, 0))).val()
    mk = BRepFilletAPI_MakeFillet(t.val().wrapped)
    mk.Add(TAB_CORNER_R, e_vert.wrapped)
    mk.Add(TAB_BOTTOM_R, e_bot.wrapped)
    mk.Build()
    solid = cq.Shape.cast(mk.Shape())
    # small round along the outer lower edge
    e_out = cq.Workplane("XY").newObject([solid]).edges("|X").edges(
        cq.selectors.NearestToPointSelector(((x0 + x1) / 2 + 2, yo, 0))).val()
    solid = solid.fillet(TAB_EDGE_R, [e_out])
    return cq.Workplane("XY").newObject([solid])


def tab_cuts(body, yc, side):
    yi = yc + side * PLATE_HW
    yo = yc + side * TAB_HW
    # transverse round snap groove, closed at the outer side
    ylip = yo - side * OUTER_LIP
    ya, yb = min(yi, ylip), max(yi, ylip)
    g = cyl_y(ya, yb, X0 + GROOVE_XC, T_TAB - GROOVE_DZ, GROOVE_R)
    body = body.cut(g)
    # small snap groove along X through the end lip
    xg = cyl_x(X0 + GROOVE_XC, X0 + L + 1,
               yc + side * XGROOVE_Y, T_TAB - XGROOVE_DZ,
               XGROOVE_R)
    body = body.cut(xg)
    return body


def channel_cut(body, yc):
    c = cyl_x(X0 + CHAN_X0, X0 + L + 1, yc, CHAN_ZC, CHAN_R)
    return body.cut(c)


def holes(body, yc):
    for s in (1, -1):
        h = (cq.Workplane("XY", origin=(X0 + HOLE_X, yc + s * HOLE_Y, -1))
             .circle(HOLE_D / 2).extrude(T_PLATE + 2))
        body = body.cut(h)
    return body


def letter_r(xc, yc):
    """Simple stroke geometry of an "R", readable from below, for engraving."""
    H, W, t = R_H, R_W, R_T
    rb = 0.28 * H                   # bowl radius
    vb = H - 2 * rb                 # bottom of the bowl
    pl = cq.Plane(origin=(xc + H / 2, yc + W / 2, R_DEPTH),
                  xDir=(0, -1, 0), normal=(0, 0, -1))
    d = R_DEPTH + 0.2

    def wp():
        return cq.Workplane(pl)

    # stem
    stem = wp().center(t / 2, H / 2).rect(t, H).extrude(d)
    # bowl: a "D" shape minus its counter
    outer = (wp().center((W - rb) / 2, H - rb).rect(W - rb, 2 * rb).extrude(d)
             .union(wp().center(W - rb, H - rb).circle(rb).extrude(d)))
    inner = (wp().center((t + W - rb) / 2, H - rb)
             .rect(W - rb - t, 2 * rb - 2 * t).extrude(d)
             .union(wp().center(W - rb, H - rb).circle(rb - t).extrude(d)))
    bowl = outer.cut(inner)
    # diagonal leg
    u0 = 0.45 * W
    leg = (wp().polyline([(u0, vb + 0.2), (u0 + 1.25 * t, vb + 0.2),
                          (W, 0), (W - 1.25 * t, 0)]).close().extrude(d))
    return stem.union(bowl).union(leg)


# ------------------------------------------------------------------
# Back body (+Y): plate with two screw holes, nut traps, trough
# ------------------------------------------------------------------
def back_body(yc):
    p = box(X0, X0 + L, yc - PLATE_HW, yc + PLATE_HW, 0, T_PLATE)
    p = p.edges("|Z").edges(cq.selectors.BoxSelector(
        (X0 - 1, yc - PLATE_HW - 1, -1), (X0 + 1, yc + PLATE_HW + 1, 10))
    ).fillet(CORNER_R)
    for s in (1, -1):
        p = p.union(tab(yc, s))
    p = holes(p, yc)
    # hex nut traps from below (they break out through the side faces)
    for s in (1, -1):
        n = (cq.Workplane("XY", origin=(X0 + HOLE_X, yc + s * HOLE_Y, -0.5))
             .polygon(6, NUT_AF / math.cos(math.pi / 6))
             .extrude(NUT_DEPTH + 0.5))
        p = p.cut(n)
    # small trough (axis along X) on top
    p = p.cut(cyl_x(X0 + TROUGH_X0, X0 + CHAN_X0 + 0.5, yc, T_PLATE,
                    TROUGH_R))
    p = channel_cut(p, yc)
    for s in (1, -1):
        p = tab_cuts(p, yc, s)
    p = p.cut(letter_r(X0 + R_XC, yc))
    return p


# ------------------------------------------------------------------
# Front body (-Y): forked plate with recessed floor
# ------------------------------------------------------------------
def front_body(yc):
    p = box(X0, X0 + L, yc - PLATE_HW, yc + PLATE_HW, 0, T_PLATE)
    # slot between the two arms
    p = p.cut(box(X0 - 1, X0 + POCKET_X0, yc - ARM_GAP_HW, yc + ARM_GAP_HW,
                  -1, T_PLATE + 1))
    # round the outer (and slightly the inner) corners of the arms
    for s in (1, -1):
        p = p.edges("|Z").edges(cq.selectors.NearestToPointSelector(
            (X0, yc + s * PLATE_HW, T_PLATE / 2))).fillet(CORNER_R)
        p = p.edges("|Z").edges(cq.selectors.NearestToPointSelector(
            (X0, yc + s * ARM_GAP_HW, T_PLATE / 2))).fillet(ARM_INNER_R)
    # recess leaving a thin floor and thin side walls
    p = p.cut(box(X0 + POCKET_X0, X0 + CHAN_X0, yc - POCKET_HW,
                  yc + POCKET_HW, FLOOR_T, T_PLATE + 1))
    for s in (1, -1):
        p = p.union(tab(yc, s))
    p = holes(p, yc)
    p = channel_cut(p, yc)
    for s in (1, -1):
        p = tab_cuts(p, yc, s)
    p = p.cut(letter_r(X0 + R_XC, yc))
    return p


back = back_body(BODY_SPACING / 2)
front = front_body(-BODY_SPACING / 2)

# the two separate bodies, kept in their relative positions
result = cq.Workplane("XY").newObject(
    [cq.Compound.makeCompound([back.val(), front.val()])])

VIEW = {"azimuth": 45, "elevation": 26}
